import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 180.0          # plate width  (X)
H = 100.0          # plate height (Z)
T = 6.4            # body thickness (Y), front face at Y=0, back at Y=T
R_TL = 32.0        # big corner radius (top-left, seen from front)
R_C = 6.0          # other corner radii
R_FRONT = 5.8      # rounding of the front perimeter edge

# stepped tongue (lip) on the back
LIP_IN = 2.4       # inset of the lip base from the outer edge
LIP_BASE_H = 1.0   # height of the lip base above the back face
TONGUE_IN = 3.0    # inset of the tongue outer face
TONGUE_H = 0.9     # tongue height above the lip base
WALL_IN = 4.2      # inset of the inner wall (pocket edge)
FLOOR = 3.0        # pocket floor (front wall thickness)

# screw boss clusters on the back
PIN_TOP = 10.4     # top of the locating pins (Y)
PIN_W = 2.4        # square locating pins
PIN_DX = 5.5
PIN_TIP_R = 0.5
PIN_DZ = 5.0
TUBE_OD = 7.6
TUBE_TOP = 6.2

# countersunk holes on the front
RING_OD = 7.4      # raised rim around each countersink
RING_H = 0.3
CSK_D = 7.4
BORE_D = 4.6
BORE_DEPTH = 4.3
THRU_D = 2.6

# raised circular feet on the front
PAD_D = 12.4
PAD_H = 0.3

# bottom notch
NOTCH_X = 8.0
NOTCH_W = 10.0
NOTCH_D = 1.2

# relief at the back of the bottom edge near the +X corner
CR_X0, CR_X1 = 78.5, 92.0
CR_D = 1.3
CR_Y0 = 4.5

# boot0 access hole
BOOT_X, BOOT_Z = -2.6, -41.2
BOOT_BOSS_TOP = 5.6
ARROW_X0, ARROW_X1 = 0.6, 4.9   # arrow from the hole towards the label
TEXT = "Boot0"
TEXT_SIZE = 4.6
TEXT_X, TEXT_Z = 11.3, -41.5

screw_pts = [(-51.7, 21.8), (10.2, 23.3), (63.5, 29.2), (-41.1, -5.6),
             (-58.2, -36.1), (16.7, -29.8), (42.1, -22.9)]
# which locating pins each cluster carries: +X, -X, +Z, -Z
cluster_pins = ["xXzZ", "xXzZ", "xXzZ", "xXz", "xXZ", "xXz", "xXzZ"]
pad_pts = [(-70.0, 31.4), (76.3, 37.0), (-77.8, -37.1), (76.3, -37.2)]
lip_gaps = [(0.0, 14.0), (-20.0, -9.0), (78.5, 83.0)]   # X ranges on bottom edge


def rrect(wp, w, h, rtl, rtr, rbr, rbl):
    """Rounded rectangle centred on the workplane origin, per-corner radii."""
    x0, x1, y0, y1 = -w / 2, w / 2, -h / 2, h / 2
    c = math.sqrt(0.5)
    p = wp.moveTo(x0 + rbl, y0).lineTo(x1 - rbr, y0)
    p = p.threePointArc((x1 - rbr + rbr * c, y0 + rbr - rbr * c), (x1, y0 + rbr))
    p = p.lineTo(x1, y1 - rtr)
    p = p.threePointArc((x1 - rtr + rtr * c, y1 - rtr + rtr * c), (x1 - rtr, y1))
    p = p.lineTo(x0 + rtl, y1)
    p = p.threePointArc((x0 + rtl - rtl * c, y1 - rtl + rtl * c), (x0, y1 - rtl))
    p = p.lineTo(x0, y0 + rbl)
    p = p.threePointArc((x0 + rbl - rbl * c, y0 + rbl - rbl * c), (x0 + rbl, y0))
    return p.close()


def outline(y, inset):
    """Plate outline offset inwards by `inset`, on a plane at depth y."""
    wp = cq.Workplane("XZ", origin=(0, y, 0))
    return rrect(wp, W - 2 * inset, H - 2 * inset,
                 R_TL - inset, R_C - inset, R_C - inset, R_C - inset)


# ---------------- main body ----------------
body = outline(0, 0).extrude(-T)
body = body.faces("<Y").edges().fillet(R_FRONT)

# stepped tongue around the back
lip_base = outline(T - 0.01, LIP_IN).extrude(-(LIP_BASE_H + 0.01))
tongue = outline(T + LIP_BASE_H - 0.01, TONGUE_IN).extrude(-(TONGUE_H + 0.01))
body = body.union(lip_base).union(tongue)

# pocket inside the tongue
pocket = outline(FLOOR, WALL_IN).extrude(-(T + LIP_BASE_H + TONGUE_H))
body = body.cut(pocket)

# gaps in the tongue along the bottom edge
for (xa, xb) in lip_gaps:
    gap = (cq.Workplane("XY")
           .box(xb - xa, LIP_BASE_H + TONGUE_H + 1, WALL_IN + 1.5)
           .translate(((xa + xb) / 2, T + (LIP_BASE_H + TONGUE_H + 1) / 2,
                       -H / 2 + (WALL_IN + 1.5) / 2 - 0.5)))
    body = body.cut(gap)

# ---------------- screw boss clusters (back) ----------------
def ycyl_s(x, z, y0, y1, d):
    return cq.Solid.makeCylinder(d / 2, y1 - y0, cq.Vector(x, y0, z), cq.Vector(0, 1, 0))


def ycone_s(x, z, y0, y1, d0, d1):
    return cq.Solid.makeCone(d0 / 2, d1 / 2, y1 - y0, cq.Vector(x, y0, z),
                             cq.Vector(0, 1, 0))


Y_BASE = FLOOR - 0.2          # features start slightly inside the floor
pin_proto = (cq.Workplane("XY").box(PIN_W, PIN_TOP - Y_BASE, PIN_W)
             .edges("|Y").fillet(0.3)
             .faces(">Y").edges().fillet(PIN_TIP_R)
             .translate((0, (PIN_TOP + Y_BASE) / 2, 0))).val()
PIN_OFFS = {"x": (PIN_DX, 0), "X": (-PIN_DX, 0), "z": (0, PIN_DZ), "Z": (0, -PIN_DZ)}

adds = []
for (cx, cz), pins in zip(screw_pts, cluster_pins):
    adds.append(ycyl_s(cx, cz, Y_BASE, TUBE_TOP, TUBE_OD))
    for key in pins:
        dx, dz = PIN_OFFS[key]
        adds.append(pin_proto.moved(cq.Location(cq.Vector(cx + dx, 0, cz + dz))))

# boot0 boss
adds.append(ycyl_s(BOOT_X, BOOT_Z, Y_BASE, BOOT_BOSS_TOP, 4.4))

# ---------------- front features ----------------
# raised feet
for (px, pz) in pad_pts:
    adds.append(ycyl_s(px, pz, -PAD_H, 0.5, PAD_D))
# raised rims around the countersinks and the boot0 hole
for (cx, cz) in screw_pts:
    adds.append(ycyl_s(cx, cz, -RING_H, 0.5, RING_OD))
adds.append(ycyl_s(BOOT_X, BOOT_Z, -RING_H, 0.5, 4.2))

# raised "Boot0" marking with an arrow pointing at the access hole
# (reads upside-down when seen from the front)
ARROW_Y0 = 0.1
adds.append(cq.Workplane("XY")
            .box(ARROW_X1 - ARROW_X0, RING_H + ARROW_Y0, 0.45)
            .translate(((ARROW_X0 + ARROW_X1) / 2, (ARROW_Y0 - RING_H) / 2, BOOT_Z))
            .val())
adds.append(cq.Workplane("XZ", origin=(0, ARROW_Y0, 0))
            .polyline([(ARROW_X0 - 1.3, BOOT_Z), (ARROW_X0 + 0.2, BOOT_Z + 0.8),
                       (ARROW_X0 + 0.2, BOOT_Z - 0.8)]).close()
            .extrude(RING_H + ARROW_Y0).val())

body = cq.Workplane().add(body.val().fuse(*adds).clean())

try:
    txt_plane = cq.Plane(origin=(TEXT_X, ARROW_Y0, TEXT_Z), xDir=(-1, 0, 0),
                         normal=(0, -1, 0))
    label = cq.Workplane(txt_plane).text(TEXT, TEXT_SIZE, RING_H + ARROW_Y0,
                                         halign="center", valign="center")
    if label.val().isValid():
        body = body.union(label)
except Exception:
    pass

# ---------------- holes and cut-outs ----------------
cuts = []
csk_depth = (CSK_D - BORE_D) / 2
y_top = -RING_H - 0.01
for (cx, cz) in screw_pts:
    cuts.append(ycone_s(cx, cz, y_top, y_top + csk_depth + 0.01, CSK_D + 0.02, BORE_D))
    cuts.append(ycyl_s(cx, cz, y_top, BORE_DEPTH, BORE_D))
    cuts.append(ycyl_s(cx, cz, -1, PIN_TOP + 1, THRU_D))

# boot0 hole
cuts.append(ycone_s(BOOT_X, BOOT_Z, -RING_H - 0.01, 1.1, 4.22, 2.0))
cuts.append(ycyl_s(BOOT_X, BOOT_Z, -1, BOOT_BOSS_TOP + 1, 2.0))

# bottom notch (through the thickness)
cuts.append(cq.Workplane("XY").box(NOTCH_W, 40, 2 * NOTCH_D)
            .edges("|Y").fillet(0.9)
            .translate((NOTCH_X, 5, -H / 2)).val())

# small relief at the back of the bottom edge near the +X corner
cuts.append(cq.Workplane("XY").box(CR_X1 - CR_X0, 12.0, 2 * CR_D)
            .translate(((CR_X0 + CR_X1) / 2, CR_Y0 + 6.0, -H / 2)).val())

body = cq.Workplane().add(body.val().cut(*cuts).clean())

result = body

VIEW = {"azimuth": 45, "elevation": 26}
